import math
import cadquery as cq

# Sheet-metal hood (guard).  It wraps around a drum at its -Y end (curved,
# slightly inclined end wall with a ledge), its top plate bends up near the
# +Y end where an inclined end plate closes it, and it is open at the bottom.
# The -X side is creased (upper panel sloping inward, lower panel almost
# vertical) and carries an outward-sloping mounting flange.  The part sits
# in its installed (slightly tilted) orientation, so every face is given as a
# plane: outward normal + a point on it.

# ---------------- driving dimensions (mm) ----------------
T = 3.0                      # sheet thickness

# main faces of the hood (outward normal, point)
TOP = ((0.1366, -0.1102, 0.9845), (67.72, 102.68, 81.38))      # top plate, flat part
STEEP = ((0.1169, -0.4485, 0.8861), (69.55, 182.85, 97.92))    # top plate, bent-up part
END = ((0.0859, 0.9192, 0.3842), (71.03, 218.5, 68.82))        # inclined +Y end plate
BOTTOM = ((-0.1139, 0.1102, -0.9874), (69.55, 142.85, 20.02))  # open bottom
WALL_R = ((0.9977, -0.0374, -0.0561), (120.18, 102.02, 49.2))  # +X side wall
UP_FLAT = ((-0.9714, 0.053, -0.2314), (16.37, 113.47, 81.57))  # -X upper panel (flat part)
UP_STEEP = ((-0.9658, 0.0375, -0.2565), (17.57, 197.77, 93.87))  # -X upper panel (bent part)
LOWER = ((-0.998, 0.0252, 0.0572), (21.35, 160.93, 46.98))     # -X lower panel
BEND_R = 25.0                # bend radius between flat and bent-up top

# curved end wall around the drum: lower part a vertical cylinder, upper part
# an inclined cylinder leaning toward the drum; they cross along a crease
LOW_C = (-54.4, -80.38)
LOW_R = 191.39
UP_BASE = (-74.72, -74.43, 0.0)
UP_AXIS = (0.1072, -0.3877, 1.0)
UP_R = 209.47

# ledge on the curved end wall
ARC_C = (-42.3, -86.8)       # centre of the ledge arc (plan view)
LEDGE_R = 163.0              # outer radius of the ledge
LEDGE_DROP = 26.5            # below the top plate
LEDGE_X0 = 19.8              # -X end of the ledge
LEDGE_A1 = 35.4              # +X end (radial cut), deg

# mounting flange on the -X side (plan outline, flange plane)
FL_PTS = [(-1.5, 171.2), (-1.0, 104.1), (13.3, 92.9), (24.0, 84.5), (24.0, 171.2)]
FL_P1, FL_P2, FL_P3 = (-1.5, 171.2, 66.5), (-1.0, 104.1, 55.6), (16.6, 171.2, 75.5)
FL_SAG = 3.0                 # the flange is slightly dished along its length

# holes
HOLE_TOP = (47.7, 99.5, 8.0)        # x, y, radius (top plate)
HOLE_LEDGE = (53.0, 55.5, 1.7)      # ledge
HOLE_FLANGE = (10.5, 132.6, 1.7)    # flange
SLOT_END = ((76.5, 227.1, 47.4), 17.0, 7.0)   # centre, length, width (end plate)

# inner Z-bracket near the +Y end: foot on the bottom edge, web, and an upper
# leg lying against the inner face of the end plate, next to the slot
BR_X = 37.0                  # web position
BR_Y0 = 203.0                # -Y end of web / foot
BR_FOOT = 8.0                # foot width (toward -X)
BR_TOP_Z = (54.0, 64.0)      # z range of the upper leg
BR_LEG_LEN = 30.0            # x length of the upper leg
BR_GAP = 0.0                 # gap between upper leg and end plate
BR_HOLE = 1.7

BIG = 1000.0


def V(*a):
    return cq.Vector(*a)


def halfspace(plane, offset=0.0):
    """solid on the outward side of a plane (normal, point); offset moves it along n"""
    n = V(*plane[0]).normalized()
    p = V(*plane[1]) + n * offset
    ref = V(0, 0, 1) if abs(n.z) < 0.9 else V(1, 0, 0)
    xd = ref.cross(n).normalized()
    pl = cq.Plane(origin=p, xDir=xd, normal=n)
    return cq.Workplane(pl).rect(BIG, BIG).extrude(BIG / 2)


def slab(plane, t0, t1):
    """region between the offsets t0 < t1 (along the outward normal) of a plane"""
    return halfspace(plane, t0).cut(halfspace(plane, t1))


def flip(plane):
    return (tuple(-c for c in plane[0]), plane[1])


def plane_z(plane, x, y):
    (nx, ny, nz), (px, py, pz) = plane
    return pz - (nx * (x - px) + ny * (y - py)) / nz


def drum(extra=0.0):
    """the space occupied by the drum (plus clearance 'extra')"""
    # oblique cylinder: horizontal circular sections, centre sliding along UP_AXIS
    z0, h = -200.0, 500.0
    c0 = V(UP_BASE[0] + UP_AXIS[0] * z0, UP_BASE[1] + UP_AXIS[1] * z0, z0)
    circ = cq.Wire.makeCircle(UP_R + extra, c0, V(0, 0, 1))
    upper = cq.Workplane("XY").add(cq.Solid.extrudeLinear(circ, [], V(UP_AXIS[0] * h, UP_AXIS[1] * h, h)))
    lower = cq.Workplane("XY").add(
        cq.Solid.makeCylinder(LOW_R + extra, 500.0, V(LOW_C[0], LOW_C[1], -200.0), V(0, 0, 1)))
    # the two surfaces cross along the crease; the drum is the common region
    return upper.intersect(lower)


def zcyl(x, y, r, z0=-100.0, h=400.0):
    return cq.Workplane("XY").add(cq.Solid.makeCylinder(r, h, V(x, y, z0), V(0, 0, 1)))


# ---------------- envelope (solid hood volume) ----------------
env = cq.Workplane("XY").box(400, 500, 400).translate((60, 110, 50))
env = env.cut(halfspace(TOP).intersect(halfspace(STEEP)))        # valley bend
env = env.cut(halfspace(END))
env = env.cut(halfspace(BOTTOM))
env = env.cut(halfspace(WALL_R))
try:  # smooth bend between the flat and bent-up parts of the top plate
    nt, ns = V(*TOP[0]), V(*STEEP[0])
    bend_edges = [
        e for e in env.edges().vals()
        if abs(e.tangentAt(0.5).dot(nt)) < 1e-3 and abs(e.tangentAt(0.5).dot(ns)) < 1e-3
    ]
    env = cq.Workplane("XY").add(env.val().fillet(BEND_R, bend_edges))
except Exception:
    pass

# -X side: creased panel; split the upper panel at the bend
nt, ns = V(*TOP[0]).normalized(), V(*STEEP[0]).normalized()
n_split = (nt - ns).normalized()                 # bisector through the bend line
p_bend = V(*STEEP[1])
# point on the bend line: intersect TOP and STEEP along x = 70
yb = p_bend.y
for _ in range(60):
    zt = plane_z(TOP, 70.0, yb)
    zs = plane_z(STEEP, 70.0, yb)
    dzt = -TOP[0][1] / TOP[0][2]
    dzs = -STEEP[0][1] / STEEP[0][2]
    yb -= (zt - zs) / (dzt - dzs)
p_split = (70.0, yb, plane_z(TOP, 70.0, yb))
split_flat = halfspace(((-n_split.x, -n_split.y, -n_split.z), p_split))
split_steep = halfspace(((n_split.x, n_split.y, n_split.z), p_split))
upper = halfspace(UP_FLAT).intersect(split_flat).union(halfspace(UP_STEEP).intersect(split_steep))
env = env.cut(upper.intersect(halfspace(LOWER)))
env_full = env

# -Y end: curved wall around the drum
env = env_full.cut(drum())

# ---------------- hollow shell, open at the bottom ----------------
nb = V(*BOTTOM[0]).normalized()
open_faces = [max((f for f in env.faces().vals() if f.geomType() == "PLANE" and f.normalAt().dot(nb) > 0.999),
                  key=lambda f: f.Area())]
shell = env.val().shell(open_faces, -T)
body = cq.Workplane("XY").add(shell)
cavity = env.cut(body)

# ---------------- ledge on the curved end wall ----------------
a1 = math.radians(LEDGE_A1)
a0 = math.radians(85.0)
am = 0.5 * (a0 + a1)
r_o = UP_R + 20.0


def pc(r, a):
    return (ARC_C[0] + r * math.cos(a), ARC_C[1] + r * math.sin(a))


sector = (
    cq.Workplane("XY")
    .moveTo(*pc(LEDGE_R, a1))
    .lineTo(*pc(r_o, a1))
    .threePointArc(pc(r_o, am), pc(r_o, a0))
    .lineTo(*pc(LEDGE_R, a0))
    .threePointArc(pc(LEDGE_R, am), pc(LEDGE_R, a1))
    .close()
    .extrude(400)
    .translate((0, 0, -100))
)
ledge = sector.intersect(slab(TOP, -LEDGE_DROP - T, -LEDGE_DROP)).intersect(drum(0.5 * T))
ledge = ledge.intersect(halfspace(((1, 0, 0), (LEDGE_X0, 0, 0))))
ledge = ledge.cut(zcyl(HOLE_LEDGE[0], HOLE_LEDGE[1], HOLE_LEDGE[2]))
body = body.union(ledge)

# ---------------- mounting flange on the -X side ----------------
f1, f2, f3 = V(*FL_P1), V(*FL_P2), V(*FL_P3)
nf = (f2 - f1).cross(f3 - f1).normalized()
if nf.z < 0:
    nf = -nf
fl_outline = cq.Workplane("XY").polyline(FL_PTS).close().extrude(400).translate((0, 0, -100))
u_fl = (f2 - f1).normalized()                  # along the outer edge
d_fl = nf.cross(u_fl).normalized()            # across the flange
half = 0.5 * (f2 - f1).Length
r_fl = half * half / (2.0 * FL_SAG) + 0.5 * FL_SAG
ax_p = (f1 + f2) * 0.5 + nf * (r_fl - FL_SAG) - d_fl * 300.0
dish = cq.Workplane("XY").add(cq.Solid.makeCylinder(r_fl + T, 600.0, ax_p, d_fl)).cut(
    cq.Workplane("XY").add(cq.Solid.makeCylinder(r_fl, 600.0, ax_p, d_fl)))
flange = fl_outline.intersect(dish).cut(cavity).cut(drum())
flange = flange.cut(zcyl(HOLE_FLANGE[0], HOLE_FLANGE[1], HOLE_FLANGE[2]))
body = body.union(flange)

# ---------------- inner Z-bracket near the +Y end ----------------
above_bottom = halfspace(flip(BOTTOM))
br_leg = (
    cq.Workplane("XY").box(BR_LEG_LEN, 80.0, BR_TOP_Z[1] - BR_TOP_Z[0], centered=False)
    .translate((BR_X, 180.0, BR_TOP_Z[0]))
    .intersect(slab(END, -(2.0 * T + BR_GAP), -(T + BR_GAP)))
)
in_front_of_leg = halfspace(flip(END), 2.0 * T + BR_GAP - 0.5)
br_web = (
    cq.Workplane("XY").box(T, 60.0, 200.0, centered=False).translate((BR_X, BR_Y0, BR_TOP_Z[1] - 200.0))
    .intersect(above_bottom).intersect(in_front_of_leg)
)
br_foot = (
    cq.Workplane("XY").box(BR_FOOT + T, 60.0, 300.0, centered=False).translate((BR_X - BR_FOOT, BR_Y0, -150.0))
    .intersect(slab(BOTTOM, -T, 0.0))
)
bracket = br_web.union(br_leg).union(br_foot)
yf = 0.5 * (BR_Y0 + 218.0)
bracket = bracket.intersect(env_full).cut(zcyl(BR_X - BR_FOOT * 0.5, yf, BR_HOLE))
body = body.union(bracket)

# ---------------- holes ----------------
body = body.cut(zcyl(HOLE_TOP[0], HOLE_TOP[1], HOLE_TOP[2], 40.0, 100.0))

ne = V(*END[0]).normalized()
sc = V(*SLOT_END[0])
xe = (V(1, 0, 0) - ne * ne.x).normalized()
slot_pl = cq.Plane(origin=sc - ne * 15.0, xDir=xe, normal=ne)
body = body.cut(cq.Workplane(slot_pl).slot2D(SLOT_END[1], SLOT_END[2]).extrude(30))

result = body
